import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 50.0          # outer radius of the dome at the rim plane
H_DOME = 31.6         # depth of the (oblate half-ellipsoid) dome below the rim plane
SHELL_T = 2.0         # wall thickness of the shell (offset of the outside)
PLATE_T = 5.5         # thickness of the top plate carrying the neck
FLARE_R = 4.0         # round on the lower edge of the neck bore

NECK_RI = 38.6        # threaded neck inner radius
NECK_RO = 42.4        # threaded neck outer radius
NECK_H = 8.2          # neck height above the rim plane
BEAD_RO = 45.2        # thread crest radius
BEAD_H = 2.3          # thread bead height
THREAD_P = 4.2        # thread pitch (single start)
THREAD_SWEEP = 350.0  # angular length of the thread (deg)
THREAD_A0 = 210.0     # angular position of the thread start (deg from +X)
THREAD_Z0 = 2.12      # height of the thread start above the rim plane

# press button: cylindrical flat on the underside (axis parallel to X)
BTN_R = 50.0
BTN_CY, BTN_CZ = 21.2, -74.2

# electronics compartment (square, walls standing in the dome)
CMP_X0, CMP_X1 = -13.4, 23.5   # inner faces, X
CMP_Y0, CMP_Y1 = -3.2, 33.6    # inner faces, Y
CMP_WALL = 2.9
CMP_TOP = -5.3        # top of the walls
CMP_FLOOR = -16.1     # compartment floor
NOTCH_Z = 3.0         # depth of the key notch at the compartment corner
NOTCH_SLOPE = 1.24    # slope of the notch floor
LIP_Y0, LIP_Y1 = 7.4, 23.7     # opening in the left wall (down to the floor)
LIP_R = 2.5
GAP_X0, GAP_X1 = -1.65, 6.3    # cable gap in the front wall / stem of the pocket
STEM_Y1 = 8.6                  # top of the pocket stem
PB_X0, PB_Y0, PB_Y1 = 2.42, 6.7, 23.4   # pocket body (button area)
PB_X1 = 23.05
PB_R = 7.0                     # rounding of the pocket body's far end
ST_X0, ST_Y0, ST_Y1 = 14.4, 22.9, 32.75  # pocket step under the light hole
WIN_X0, WIN_X1 = 8.5, 17.4     # window in the front wall
WIN_Z0, WIN_Z1 = -15.0, -11.6

# flexure in the button skin
U_CX, U_CY = 14.4, 15.05       # centre of the U-slot round end
U_R = 6.1             # U-slot centre-line radius
U_X0 = 5.9            # open end of the U arms
U_W = 0.7             # slot width
NUB_X, NUB_Y, NUB_R = 13.35, 15.25, 2.72
NUB_TOP = -17.5
HOLE_X, HOLE_Y, HOLE_R = 18.65, 31.0, 1.5

# battery clips (elliptical ring of four arcs following the shell)
CL_CY = -24.55
CL_A, CL_B = 20.3, 13.55       # outer semi-axes
CL_T = 2.0
CL_H = 3.5            # clip height above the seat
CL_TILT = 22.0        # seat plane tilt (deg), leaning towards +Y like the shell
CL_Z0 = -22.9         # seat height at the ring centre
CL_GAP_X = 2.8
CL_GAP_Y = 2.95

SEAM_ANGLE = 90.0     # where the seam of the outer revolved faces is put (+Y, through the button flat)
CAV_SEAM_ANGLE = 45.0 # seam of the cavity faces (hidden behind the compartment)

VIEW = {"azimuth": 45, "elevation": 26}


# ---------------- helpers ----------------
def half_ellipsoid(a, c, z_top=0.0):
    """Solid lower half of an oblate ellipsoid (semi-axes a, a, c) centred at origin, truncated at z_top."""
    s = (
        cq.Workplane("XZ")
        .moveTo(0, 0)
        .lineTo(a, 0)
        .ellipseArc(a, c, angle1=270, angle2=360, sense=-1, startAtCurrent=True)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
    )
    if z_top < 0:
        s = s.cut(cq.Workplane("XY").box(4 * a, 4 * a, 4 * c, centered=(True, True, False)).translate((0, 0, z_top)))
    return s


def zbox(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False).translate((x0, y0, z0))


def x_cylinder(r, cy, cz):
    return cq.Workplane("YZ").circle(r).extrude(2 * R_OUT + 10).translate((-R_OUT - 5, cy, cz))


# ---------------- outer body ----------------
dome = half_ellipsoid(R_OUT, H_DOME)
neck = cq.Workplane("XY").circle(NECK_RO).extrude(NECK_H).rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
# single-turn helical thread bead with a rounded crest
r_root = NECK_RO - 0.6
helix = cq.Wire.makeHelix(
    pitch=THREAD_P,
    height=THREAD_P * THREAD_SWEEP / 360.0,
    radius=r_root,
    center=cq.Vector(0, 0, THREAD_Z0),
    dir=cq.Vector(0, 0, 1),
)
bead = (
    cq.Workplane("XZ", origin=(0, 0, THREAD_Z0))
    .moveTo(r_root, -BEAD_H / 2)
    .lineTo(BEAD_RO - BEAD_H / 2, -BEAD_H / 2)
    .threePointArc((BEAD_RO, 0), (BEAD_RO - BEAD_H / 2, BEAD_H / 2))
    .lineTo(r_root, BEAD_H / 2)
    .close()
    .sweep(cq.Workplane().add(helix), isFrenet=True)
    .rotate((0, 0, 0), (0, 0, 1), THREAD_A0)
)
btn_cut = x_cylinder(BTN_R, BTN_CY, BTN_CZ)
body = dome.union(neck).union(bead).cut(btn_cut)

# envelope 0.5 mm inside the outside, used to trim internal features so they never break the skin
env = half_ellipsoid(R_OUT - 0.5, H_DOME - 0.5).cut(x_cylinder(BTN_R + 0.5, BTN_CY, BTN_CZ))

# ---------------- cavity: shell offset of the outside + neck bore with rounded lower edge ----------------
a_i, c_i = R_OUT - SHELL_T, H_DOME - SHELL_T
z_pl = -PLATE_T
r_e = a_i * math.sqrt(1.0 - (z_pl / c_i) ** 2)
th_e = 360.0 - math.degrees(math.atan2(-z_pl / c_i, r_e / a_i))
cavity = (
    cq.Workplane("XZ")
    .moveTo(0, NECK_H + 1)
    .lineTo(NECK_RI, NECK_H + 1)
    .lineTo(NECK_RI, z_pl + FLARE_R)
    .threePointArc(
        (NECK_RI + FLARE_R * (1 - math.sqrt(0.5)), z_pl + FLARE_R * (1 - math.sqrt(0.5))),
        (NECK_RI + FLARE_R, z_pl),
    )
    .lineTo(r_e, z_pl)
    .ellipseArc(a_i, c_i, angle1=270, angle2=th_e, sense=-1, startAtCurrent=True)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), CAV_SEAM_ANGLE)
)
cavity = cavity.cut(x_cylinder(BTN_R + SHELL_T, BTN_CY, BTN_CZ))
body = body.cut(cavity)

# ---------------- compartment ----------------
ox0, ox1 = CMP_X0 - CMP_WALL, CMP_X1 + CMP_WALL
oy0, oy1 = CMP_Y0 - CMP_WALL, CMP_Y1 + CMP_WALL
block = zbox(ox0, ox1, oy0, oy1, -H_DOME - 1, CMP_TOP).intersect(env)
body = body.union(block)
# hollow the compartment down to the floor
body = body.cut(zbox(CMP_X0, CMP_X1, CMP_Y0, CMP_Y1, CMP_FLOOR, CMP_TOP + 1))

# wedge-shaped key notch in the neck bore, in line with the compartment corner
nx0 = CMP_X1 - (NECK_H - NOTCH_Z) / NOTCH_SLOPE - 2.0
notch = (
    cq.Workplane("XZ", origin=(0, CMP_Y1, 0))
    .polyline([(CMP_X1, NECK_H + 3), (CMP_X1, NOTCH_Z), (nx0, NOTCH_Z + (CMP_X1 - nx0) * NOTCH_SLOPE)])
    .close()
    .extrude(10)
)
body = body.cut(notch)

# opening in the left wall, rounded into the floor
lip_cut = (
    cq.Workplane("YZ")
    .rect(LIP_Y1 - LIP_Y0, 30, centered=False)
    .extrude(CMP_WALL + 2)
    .translate((ox0 - 1, LIP_Y0, CMP_FLOOR))
    .edges("|X and <Z")
    .fillet(LIP_R)
)
body = body.cut(lip_cut)

# cable gap through the front wall
body = body.cut(zbox(GAP_X0, GAP_X1, oy0 - 1, CMP_Y0 + 0.1, CMP_FLOOR, NECK_H))
# window in the front wall
body = body.cut(zbox(WIN_X0, WIN_X1, oy0 - 1, CMP_Y0 + 0.1, WIN_Z0, WIN_Z1))

# P-shaped opening in the floor down to the button skin
zb, zt = -H_DOME - 1, CMP_FLOOR + 0.01
p_prism = (
    zbox(GAP_X0, GAP_X1, oy0 - 0.5, STEM_Y1, zb, zt)
    .union(zbox(PB_X0, GAP_X1 + 0.1, STEM_Y1 - 0.1, PB_Y1, zb, zt))
    .union(zbox(GAP_X1, PB_X1, PB_Y0, PB_Y1, zb, zt).edges("|Z and >X").fillet(PB_R))
    .union(zbox(ST_X0, PB_X1, ST_Y0, ST_Y1, zb, zt))
)
body = body.cut(p_prism.intersect(cavity))

# U-shaped flexure slot through the skin
u_slot = (
    cq.Workplane("XY")
    .moveTo(U_X0, U_CY + U_R)
    .lineTo(U_CX, U_CY + U_R)
    .threePointArc((U_CX + U_R, U_CY), (U_CX, U_CY - U_R))
    .lineTo(U_X0, U_CY - U_R)
    .offset2D(U_W / 2)
    .extrude(CMP_FLOOR + H_DOME + 2)
    .translate((0, 0, -H_DOME - 2))
)
body = body.cut(u_slot)

# actuator nub on the flexure
nub = cq.Workplane("XY").circle(NUB_R).extrude(20).translate((NUB_X, NUB_Y, NUB_TOP - 20)).intersect(env)
body = body.union(nub)

# small light hole
body = body.cut(cq.Workplane("XY").circle(HOLE_R).extrude(40).translate((HOLE_X, HOLE_Y, -H_DOME - 5)))

# ---------------- battery seat + clips (on a plane tilted to follow the shell) ----------------
th = math.radians(CL_TILT)
seat_pl = cq.Plane(origin=(0, CL_CY, CL_Z0), xDir=(1, 0, 0), normal=(0, math.sin(th), math.cos(th)))
cl_b = CL_B / math.cos(th)               # semi-axis measured in the tilted plane
seat = (
    cq.Workplane(seat_pl).ellipse(CL_A, cl_b).extrude(-12)
    .union(cq.Workplane(seat_pl).center(0, -cl_b - 0.5).rect(2 * CL_GAP_X, 3.0).extrude(-12))
    .intersect(env)
)
ring = (
    cq.Workplane(seat_pl).ellipse(CL_A, cl_b).ellipse(CL_A - CL_T, cl_b - CL_T).extrude(CL_H)
    .cut(cq.Workplane(seat_pl).rect(2 * CL_GAP_X, 4 * cl_b).extrude(CL_H + 1))
    .cut(cq.Workplane(seat_pl).rect(4 * CL_A, 2 * CL_GAP_Y).extrude(CL_H + 1))
)
body = body.union(seat).union(ring)

result = body
